import cadquery as cq

# ---------------------------------------------------------------- parameters
PLATE = 100.0          # square plate side (mm)
T = 1.75               # plate thickness (mm)
PITCH_X = 7.27         # letter grid pitch along X
PITCH_Y = 7.24         # letter grid pitch along Y
GRID_DX = 0.07         # small offset of the letter grid from the plate centre
GRID_DY = 0.07
HC = 4.2               # window / cap height of the letters
E = 0.06               # overshoot of glyph strokes past the window edges
SV = 1.45              # vertical stem width
TOOL_Z0 = -1.0
TOOL_H = T + 2.0

LETTERS = ["ABCD", "EFGH", "IJKL", "MNOP"]

# window width of every letter (mm)
WIDTH = {
    "A": 6.0, "B": 5.82, "C": 6.08, "D": 6.12,
    "E": 5.74, "F": 5.11, "G": 6.41, "H": 6.2,
    "I": 3.35, "J": 5.35, "K": 6.62, "L": 5.53,
    "M": 7.13, "N": 6.46, "O": 6.33, "P": 5.7,
}


# ---------------------------------------------------------------- 2D helpers
def _wp():
    return cq.Workplane("XY").workplane(offset=TOOL_Z0)


def poly(pts):
    return _wp().polyline(pts).close().extrude(TOOL_H)


def rect(x0, y0, x1, y1):
    return _wp().center((x0 + x1) / 2, (y0 + y1) / 2).rect(abs(x1 - x0), abs(y1 - y0)).extrude(TOOL_H)


def ell(cx, cy, a, b):
    return _wp().center(cx, cy).ellipse(a, b).extrude(TOOL_H)


def path(start, segs):
    """closed profile: segs are ('l', (x, y)) or ('a', (xm, ym), (x, y))"""
    w = _wp().moveTo(*start)
    for s in segs:
        if s[0] == "l":
            w = w.lineTo(*s[1])
        else:
            w = w.threePointArc(s[1], s[2])
    return w.close().extrude(TOOL_H)


def rrect(x0, y0, x1, y1, r):
    """rectangle with all four vertical edges rounded by r"""
    return rect(x0, y0, x1, y1).edges("|Z").fillet(r)


def union(*objs):
    r = objs[0]
    for o in objs[1:]:
        r = r.union(o)
    return r


# ---------------------------------------------------------------- glyphs
# every glyph lives in a window [0, W] x [0, HC]; returns the letter material
def glyph(ch, W):
    H = HC
    top, bot = H + E, -E
    if ch == "A":
        outer = poly([(0.02 * W - E, bot), (0.32 * W, bot), (0.35 * W, 0.12 * H), (0.65 * W, 0.12 * H),
                      (0.68 * W, bot), (0.98 * W + E, bot), (0.69 * W, top), (0.31 * W, top)])
        hole = poly([(0.395 * W, 0.33 * H), (0.605 * W, 0.33 * H), (0.5 * W, 0.74 * H)])
        return outer.cut(hole)
    if ch == "B":
        m = 0.65
        s = m + SV
        upper = rrect(m - 1.0, 2.4, 4.68, top, 0.6)
        lower = rrect(m - 1.0, bot, 4.8, 2.4, 0.7)
        body = union(upper, lower, rect(m, bot, s, top)).intersect(rect(m, -1, W, H + 1))
        h1 = rrect(2.1, 2.9, 3.35, 3.5, 0.28)
        h2 = rrect(2.05, 0.7, 3.6, 1.8, 0.45)
        return body.cut(h1).cut(h2)
    if ch == "C":
        xr = 4.85
        outer = rrect(0.6, -0.08, 5.7, H + 0.08, 1.45)
        ring = outer.intersect(rect(0, -1, xr, H + 1))
        ring = ring.cut(ell(3.2, H / 2, 1.15, 1.42)).cut(rect(3.2, 1.5, xr + 1, 2.7))
        return ring
    if ch == "D":
        m = 0.6
        outer = rrect(m - 1.5, bot, 5.25, top, 1.35).intersect(rect(m, -1, W, H + 1))
        hole = union(rect(2.3, 0.8, 3.0, H - 0.8), rrect(2.3, 0.8, 3.65, H - 0.8, 0.65))
        return outer.cut(hole)
    if ch == "E":
        m, s, xe = 0.78, 2.35, 4.84
        return poly([(m, bot), (m, top), (xe, top), (xe, 3.75), (s, 3.75), (s, 2.45), (xe - 0.1, 2.45),
                     (xe - 0.1, 1.95), (s, 1.95), (s, 0.75), (xe, 0.75), (xe, bot)])
    if ch == "F":
        m, s, xe = 0.78, 2.25, 4.3
        return poly([(m, bot), (m, top), (xe, top), (xe, 3.8), (s, 3.8), (s, 2.7), (xe - 0.1, 2.7),
                     (xe - 0.1, 1.85), (s, 1.85), (s, bot)])
    if ch == "G":
        xr = 5.2
        outer = rrect(0.7, -0.08, 5.9, H + 0.08, 1.5)
        ring = outer.intersect(rect(0, -1, xr, H + 1)).cut(ell(3.35, H / 2, 1.15, 1.42))
        ring = ring.cut(rect(3.3, 2.55, xr + 1, 3.15))
        bar = rect(3.6, 1.9, xr, 2.55)
        spur = rect(4.0, -1, xr, 2.55).intersect(outer)
        return union(ring, bar, spur)
    if ch == "H":
        m, w = 0.62, 1.7
        return union(rect(m, bot, m + w, top), rect(W - m - w, bot, W - m, top),
                     rect(m + w / 2, 1.5, W - m - w / 2, 2.72))
    if ch == "I":
        m = 0.95
        return rect(m, bot, W - m, top)
    if ch == "J":
        xs0, xs1, m = 2.95, 4.6, 0.55
        stem = rect(xs0, 0.9, xs1, top)
        hook = rrect(m, bot, xs1, 2.2, 1.0).intersect(rect(0, -1, W, 1.65))
        hook = hook.cut(ell(2.4, 1.75, 0.9, 1.0))
        return union(stem, hook)
    if ch == "K":
        m = 0.9
        s = 2.6
        return poly([(m, bot), (m, top), (s, top), (s, 2.97), (3.78, top), (6.05, top), (4.41, 2.6),
                     (6.2, bot), (4.16, bot), (3.15, 1.73), (s, 1.2), (s, bot)])
    if ch == "L":
        m = 0.84
        return poly([(m, bot), (m, top), (m + SV, top), (m + SV, 0.7), (4.5, 0.7), (4.5, bot)])
    if ch == "M":
        m = 0.84
        c = W / 2
        return poly([(m, bot), (m, top), (2.78, top), (c, 1.77), (W - 2.78, top), (W - m, top),
                     (W - m, bot), (W - m - 1.26, bot), (W - m - 1.26, 2.62), (W - 3.08, bot),
                     (3.08, bot), (m + 1.26, 2.62), (m + 1.26, bot)])
    if ch == "N":
        ml, mr, sr, a = 0.75, 0.7, W - 2.3, 2.7
        return poly([(ml, bot), (ml, top), (a, top), (sr, 1.93), (sr, top), (W - mr, top),
                     (W - mr, bot), (W - a, bot), (W - sr, H - 1.93), (W - sr, bot)])
    if ch == "O":
        return rrect(0.65, -0.08, W - 0.65, H + 0.08, 1.4).cut(ell(W / 2, H / 2, 1.05, 1.35))
    if ch == "P":
        m, xr, yb = 0.9, 4.76, 1.35
        s = m + SV
        rx, ry = 2.0, 1.25
        bowl = union(rect(m, yb, xr - rx, yb + ry), ell(xr - rx, yb + ry, rx, ry),
                     rrect(m - 1.5, 2.2, xr, top, 0.5)).intersect(rect(m, -1, xr, H + 1))
        body = union(bowl, rect(m, bot, s, top))
        hole = rrect(2.5, 2.55, 3.6, 3.47, 0.42)
        return body.cut(hole)
    raise ValueError(ch)


# ---------------------------------------------------------------- build
plate = cq.Workplane("XY").box(PLATE, PLATE, T, centered=(True, True, False))

cuts = None
for r, row in enumerate(LETTERS):
    cy = (1.5 - r) * PITCH_Y + GRID_DY
    for c, ch in enumerate(row):
        cx = (c - 1.5) * PITCH_X + GRID_DX
        W = WIDTH[ch]
        window = rect(0, 0, W, HC)
        piece = window.cut(glyph(ch, W)).translate((cx - W / 2, cy - HC / 2, 0))
        cuts = piece if cuts is None else cuts.union(piece)

result = plate.cut(cuts)

VIEW = {"azimuth": 45, "elevation": 26}
